"""Sheet-metal cover / tray lid.

A flat top plate with its two short sides (+/-X) bent down 90 deg into side flanges
(inner bend radius RI), the back edge (+Y) closed by an end wall, the front (-Y)
left open.  A short round pin sits in the inner corner of each side bend, close to
the open front edge.
"""
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 400.0      # overall length along X (outer faces of the two side flanges)
W = 244.0      # overall depth along Y (open front edge -> closed back wall)
H = 35.0       # overall height along Z
T = 3.3        # sheet thickness
RI = 3.9       # inner bend radius of the side flanges
RO = RI + T    # outer bend radius

PIN_R = RI       # radius of the short pins lying in the inner bend corners
PIN_Y0 = 10.0    # pin start, measured back from the open front edge
PIN_LEN = 27.0   # pin length along Y

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived profile coordinates ----------------
xo = L / 2.0          # outer face of a side flange
xi = L / 2.0 - T      # inner face of a side flange
xc = L / 2.0 - RO     # bend axis x
zc = H - RO           # bend axis z
k = 0.70710678118654752  # cos 45 deg (arc mid points)

# ---------------- U-channel: top plate + two bent side flanges ----------------
# cross-section drawn in the XZ plane (local x = X, local y = Z), extruded along Y
u_profile = (
    cq.Workplane("XZ")
    .moveTo(-xo, 0)
    .lineTo(-xo, zc)
    .threePointArc((-xc - RO * k, zc + RO * k), (-xc, H))     # outer bend, -X side
    .lineTo(xc, H)
    .threePointArc((xc + RO * k, zc + RO * k), (xo, zc))      # outer bend, +X side
    .lineTo(xo, 0)
    .lineTo(xi, 0)
    .lineTo(xi, zc)
    .threePointArc((xc + RI * k, zc + RI * k), (xc, H - T))   # inner bend, +X side
    .lineTo(-xc, H - T)
    .threePointArc((-xc - RI * k, zc + RI * k), (-xi, zc))    # inner bend, -X side
    .lineTo(-xi, 0)
    .close()
)
# Workplane("XZ") has its normal along -Y: extrude W toward -Y starting from y = +W/2
channel = u_profile.extrude(W).translate((0, W / 2.0, 0))

# ---------------- closed back wall at +Y (fills the channel opening, thickness T) ----------------
back_wall = (
    cq.Workplane("XZ")
    .moveTo(-xi, 0)
    .lineTo(-xi, zc)
    .threePointArc((-xc - RI * k, zc + RI * k), (-xc, H - T))
    .lineTo(xc, H - T)
    .threePointArc((xc + RI * k, zc + RI * k), (xi, zc))
    .lineTo(xi, 0)
    .close()
    .extrude(T)
    .translate((0, W / 2.0, 0))
)

# ---------------- short pins in the two inner bend corners near the open front ----------------
pins = (
    cq.Workplane("XZ")
    .pushPoints([(-xc, zc), (xc, zc)])   # on the bend axes
    .circle(PIN_R)
    .extrude(-PIN_LEN)                   # negative -> toward +Y
    .translate((0, -W / 2.0 + PIN_Y0, 0))
)

result = channel.union(back_wall).union(pins).clean()
